import math
import numpy as np
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm).  The plan-view geometry is laid out in "layout
# units" (x to the right, y downwards) and scaled into millimetres with S.
# ---------------------------------------------------------------------------
S = 0.5                 # mm per layout unit
CX, CY = 130.0, 388.0   # layout origin (centre of the plate)

T = 15.3 * S            # plate thickness
EDGE_CH = 1.4 * S       # chamfer on the top edges of plate and pockets
BOSS_R = 8.3 * S        # raised boss radius
BOSS_H = 7.8 * S        # raised boss height above plate
BOSS_FIL = 2.5 * S      # fillet at the foot of the raised bosses
PIN_R = 5.1 * S         # locating pin radius
PIN_H = 8.4 * S         # pin height above its boss
PIN_CH = 1.6 * S        # chamfer on the pin tip
TAB_HOLE_R = 5.8 * S    # holes in the two rear tabs
TAB_CH_RUN = 10.0 * S   # chamfer on the tab ends (horizontal run)
TAB_CH_H = 9.9 * S      # chamfer on the tab ends (height)
BIG_BOSS_R = 13.0 * S   # flush boss protruding at the front edge
BIG_CB_R = 9.6 * S      # its counterbore
BIG_HOLE_R = 6.0 * S    # its through hole
CB_DEPTH = 10.0 * S     # counterbore depth (big boss and centre hole)
CTR_CB_R = 9.5 * S      # centre counterbore
CTR_HOLE_R = 5.75 * S   # centre through hole
CTR_CH = 1.1 * S        # chamfer on the centre counterbore
GROOVE_W = 12.0 * S     # two grooves under the tail
GROOVE_GAP = 1.5 * S
GROOVE_END = 2.5 * S
GROOVE_D = 8.2 * S
HOLE2_R = 5.6 * S       # boss 2 / boss 4 bore from the top
HOLE4_R = 5.6 * S
UNDER_CB_R = 7.5 * S    # counterbore from underneath (boss 2 / boss 4)
UNDER_CB_D = 10.0 * S
HOLE3_R = 3.9 * S       # boss 3: through hole ...
CSK3_R = 6.9 * S        # ... with a 90 deg countersink at its mouth


def P(x, y):
    """layout unit (x right, y down) -> world mm (X right, Y up)"""
    return ((x - CX) * S, (CY - y) * S)


def rounded_poly(pts, z0=0.0):
    """Closed outline through layout points.  Entries are (x, y, r): a corner
    rounded with radius r (layout units), or ("spline", [(x, y), ...]): a
    smooth curve from the previous corner to the next one through the listed
    points (corners next to a spline must have r = 0).
    Returns a Workplane holding the closed wire."""
    corners = []
    for i, e in enumerate(pts):
        if isinstance(e[0], str):
            corners.append(("spline", [P(*q) for q in e[1]]))
            continue
        p = np.array(P(e[0], e[1]))
        r = e[2] * S
        if r <= 1e-9:
            corners.append((p, None, p))
            continue
        n = len(pts)
        a = np.array(P(pts[i - 1][0], pts[i - 1][1]))
        b = np.array(P(pts[(i + 1) % n][0], pts[(i + 1) % n][1]))
        v1 = (a - p) / np.linalg.norm(a - p)
        v2 = (b - p) / np.linalg.norm(b - p)
        th = math.acos(max(-1.0, min(1.0, float(np.dot(v1, v2)))))
        d = r / math.tan(th / 2)
        t1 = p + v1 * d
        t2 = p + v2 * d
        bis = (v1 + v2) / np.linalg.norm(v1 + v2)
        c = p + bis * (r / math.sin(th / 2))
        m = c - bis * r
        corners.append((t1, m, t2))
    n = len(corners)
    wp = cq.Workplane("XY", origin=(0, 0, z0)).moveTo(*corners[0][2])
    for i in range(1, n + 1):
        cnr = corners[i % n]
        if isinstance(cnr[0], str):
            continue
        prev = corners[(i - 1) % n]
        if isinstance(prev[0], str):
            # tangent continuous with the straight edge it starts from
            p0 = np.array(corners[(i - 2) % n][2])
            pp = corners[(i - 3) % n]
            q0 = np.array(pp[2]) if not isinstance(pp[0], str) else p0
            t0 = p0 - q0
            t0 = t0 / np.linalg.norm(t0)
            pts_s = [tuple(q) for q in prev[1]] + [(float(cnr[0][0]), float(cnr[0][1]))]
            nx = corners[(i + 1) % n]
            if isinstance(nx[0], str):
                t1 = np.array(pts_s[-1]) - np.array(pts_s[-2])
            else:
                t1 = np.array(nx[0]) - np.array(pts_s[-1])
            t1 = t1 / np.linalg.norm(t1)
            wp = wp.spline(pts_s, tangents=[tuple(t0), tuple(t1)], includeCurrent=True)
        else:
            wp = wp.lineTo(float(cnr[0][0]), float(cnr[0][1]))
        t1, m, t2 = cnr
        if m is not None:
            wp = wp.threePointArc((float(m[0]), float(m[1])),
                                  (float(t2[0]), float(t2[1])))
    return wp.close()


# ---------------------------------------------------------------------------
# Plate outline (layout units, r = corner radius)
# ---------------------------------------------------------------------------
OUTLINE = [
    (51.06, 318.46, 0.0),   # tab A tip
    (70.77, 316.35, 0.0),   # tab A plan chamfer end
    (87.12, 323.75, 0.0),   # notch behind tab A
    (104.64, 300.93, 2.0),  # rear corner (pin boss)
    (155.40, 327.30, 0.0),
    (188.10, 321.20, 2.0),
    (211.20, 331.50, 2.0),
    (214.60, 354.60, 6.0),
    (200.40, 416.50, 0.0),
    (207.30, 433.50, 0.0),  # tail root
    (247.80, 455.10, 2.0),  # tail end
    (235.10, 478.20, 2.0),  # tail end
    (217.20, 469.20, 0.0),  # start of the sweeping front curve
    ("spline", [(196.3, 458.0), (180.5, 450.9), (165.0, 448.0),
                (150.5, 450.0), (138.0, 454.3)]),
    (128.00, 460.00, 0.0),  # (inside the big front boss)
    (82.09, 477.06, 11.5),  # lobe around boss 4
    (27.68, 448.72, 2.5),   # front-left corner
    (36.25, 420.38, 0.0),   # root of tab B
    (20.87, 412.21, 0.0),   # tab B plan chamfer
    (11.25, 393.94, 0.0),   # tab B tip
    (17.50, 383.37, 0.0),   # tab B tip
    (47.31, 398.27, 0.0),   # notch between tabs
    (74.13, 345.38, 0.0),   # root of tab A
    (45.29, 330.48, 0.0),   # tab A tip
]

POCKETS = [
    # large lightening pocket (front-left)
    [(62.0, 379.0, 5.0), (113.2, 403.6, 3.5), (91.5, 447.5, 3.0),
     (79.0, 447.8, 4.0), (69.5, 453.0, 3.5), (60.8, 448.0, 3.0),
     (66.0, 429.0, 14.0), (59.8, 398.0, 20.0)],
    # small pocket left of the centre hole
    [(73.0, 360.5, 9.0), (89.0, 361.0, 5.0), (97.0, 372.0, 7.0),
     (109.5, 376.5, 4.0), (110.0, 391.0, 3.0), (75.5, 377.8, 5.0)],
    # triangular pocket
    [(120.3, 406.3, 3.5), (149.3, 419.6, 3.5), (102.8, 435.9, 3.5)],
    # large rounded pocket (right)
    [(147.3, 350.0, 7.5), (165.5, 377.0, 6.0), (146.5, 412.0, 4.0),
     (122.8, 398.0, 4.0)],
]

# bent (chevron) slot beside the centre hole: centre line + width
KIDNEY = [(126.0, 340.0), (133.0, 352.5), (124.1, 369.9)]
KIDNEY_W = 9.5
KIDNEY_BEND_R = 14.0

# straight slots: centre, overall length, width, angle in layout (deg, y down)
SLOTS = [
    ((129.8, 321.4), 23.0, 7.0, 23.0),
    ((193.0, 339.5), 26.0, 10.0, 29.5),
]

TAB_HOLES = [(69.8, 328.6), (30.5, 403.6)]
CTR_HOLE = (106.0, 354.75)
BIG_BOSS = (125.2, 466.0)
PIN_BOSS = (107.2, 314.8)
BOSS2 = (150.9, 338.0)
BOSS3 = (40.6, 442.4)
BOSS4 = (84.2, 465.2)

# tab end chamfers: bottom end-line endpoints and inward axis (layout)
TAB_ENDS = [
    ((45.29, 330.48), (51.06, 318.46)),
    ((17.50, 383.37), (11.25, 393.94)),
]
TAIL_END = ((247.8, 455.1), (235.1, 478.2))


# ---------------------------------------------------------------------------
# Base plate
# ---------------------------------------------------------------------------
plate = rounded_poly(OUTLINE).extrude(T)
outline_prism = rounded_poly(OUTLINE, z0=-1.0).extrude(T + BOSS_H + 10.0)

for pk in POCKETS:
    plate = plate.cut(rounded_poly(pk, z0=-1.0).extrude(T + 2.0))

# kidney slot: slot of width KIDNEY_W bent round KIDNEY_BEND_R
def bent_slot(A, B, C, rb, w):
    A, B, C = (np.array(P(*q)) for q in (A, B, C))
    h = w / 2
    d1 = (B - A) / np.linalg.norm(B - A)
    d2 = (C - B) / np.linalg.norm(C - B)
    n1 = np.array([-d1[1], d1[0]])
    n2 = np.array([-d2[1], d2[0]])
    v1, v2 = -d1, d2
    th = math.acos(max(-1.0, min(1.0, float(np.dot(v1, v2)))))
    dd = rb / math.tan(th / 2)
    t1, t2 = B + v1 * dd, B + v2 * dd
    bis = (v1 + v2) / np.linalg.norm(v1 + v2)
    cb = B + bis * (rb / math.sin(th / 2))
    um = (B - cb) / np.linalg.norm(B - cb)
    inner_left = np.dot(n1, cb - t1) > 0
    r_left = rb - h if inner_left else rb + h
    r_right = rb + h if inner_left else rb - h
    f = lambda q: (float(q[0]), float(q[1]))
    wp = (cq.Workplane("XY", origin=(0, 0, -1.0))
          .moveTo(*f(A + n1 * h))
          .lineTo(*f(t1 + n1 * h))
          .threePointArc(f(cb + um * r_left), f(t2 + n2 * h))
          .lineTo(*f(C + n2 * h))
          .threePointArc(f(C + d2 * h), f(C - n2 * h))
          .lineTo(*f(t2 - n2 * h))
          .threePointArc(f(cb + um * r_right), f(t1 - n1 * h))
          .lineTo(*f(A - n1 * h))
          .threePointArc(f(A - d1 * h), f(A + n1 * h))
          .close())
    return wp


plate = plate.cut(bent_slot(KIDNEY[0], KIDNEY[1], KIDNEY[2],
                            KIDNEY_BEND_R * S, KIDNEY_W * S).extrude(T + 2.0))

# small chamfer on the top edges of the pockets and of the front-facing
# part of the outline (the rear / right-hand edges stay sharp)
FRONT_MIN_Y = (CY - 425.0) * S     # only outline edges in front of this Y
top_face = plate.faces(">Z").val()
body = plate.val()
ch_edges = []
for w in top_face.innerWires():
    ch_edges.extend(w.Edges())
for e in top_face.outerWire().Edges():
    m = e.positionAt(0.5)
    t = e.tangentAt(0.5)
    n = cq.Vector(-t.y, t.x, 0.0)
    probe = cq.Vector(m.x + 0.05 * n.x, m.y + 0.05 * n.y, T / 2)
    if body.isInside(probe):
        n = cq.Vector(-n.x, -n.y, 0.0)
    if n.y < -0.25 and m.y < FRONT_MIN_Y:
        ch_edges.append(e)
plate = cq.Workplane("XY").add(body.chamfer(EDGE_CH, None, ch_edges))

for (c, L, W, ang) in SLOTS:
    cx, cy = P(*c)
    sl = (cq.Workplane("XY", origin=(0, 0, -1.0)).center(cx, cy)
          .slot2D(L * S, W * S, -ang).extrude(T + 2.0))
    plate = plate.cut(sl)

# ---------------------------------------------------------------------------
# Bosses
# ---------------------------------------------------------------------------
bx, by = P(*BIG_BOSS)
plate = plate.union(cq.Workplane("XY").center(bx, by).circle(BIG_BOSS_R).extrude(T))


def raised_boss(xy):
    f = BOSS_FIL
    r = BOSS_R
    c45 = math.sqrt(0.5)
    prof = (cq.Workplane("XZ")
            .moveTo(0, T - 1.0)
            .lineTo(r + f, T - 1.0)
            .lineTo(r + f, T)
            .threePointArc((r + f - c45 * f, T + f - c45 * f), (r, T + f))
            .lineTo(r, T + BOSS_H)
            .lineTo(0, T + BOSS_H)
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))
    x, y = P(*xy)
    return prof.translate((x, y, 0)).intersect(outline_prism)


for b in (PIN_BOSS, BOSS2, BOSS3, BOSS4):
    plate = plate.union(raised_boss(b))

# locating pin
px_, py_ = P(*PIN_BOSS)
pin = (cq.Workplane("XY", origin=(0, 0, T + BOSS_H - 0.2)).center(px_, py_)
       .circle(PIN_R).extrude(PIN_H + 0.2).faces(">Z").edges().chamfer(PIN_CH))
plate = plate.union(pin)

# ---------------------------------------------------------------------------
# Holes
# ---------------------------------------------------------------------------
TOP = T + BOSS_H


def cyl(xy, r, z0, h):
    x, y = P(*xy)
    return cq.Workplane("XY", origin=(0, 0, z0)).center(x, y).circle(r).extrude(h)


def cone(xy, r_bot, r_top, z0, h):
    x, y = P(*xy)
    return cq.Workplane("XY").add(
        cq.Solid.makeCone(r_bot, r_top, h, cq.Vector(x, y, z0), cq.Vector(0, 0, 1)))


for h in TAB_HOLES:
    plate = plate.cut(cyl(h, TAB_HOLE_R, -1, T + 2))

# centre counterbored hole
plate = plate.cut(cyl(CTR_HOLE, CTR_HOLE_R, -1, T + 2))
plate = plate.cut(cyl(CTR_HOLE, CTR_CB_R, T - CB_DEPTH, CB_DEPTH + 1))
plate = plate.cut(cone(CTR_HOLE, CTR_CB_R, CTR_CB_R + CTR_CH + 0.6, T - CTR_CH, CTR_CH + 0.6))

# big flush boss: counterbore + through hole
plate = plate.cut(cyl(BIG_BOSS, BIG_HOLE_R, -1, T + 2))
plate = plate.cut(cyl(BIG_BOSS, BIG_CB_R, T - CB_DEPTH, CB_DEPTH + 1))

# raised bosses
for xy, hr in ((BOSS2, HOLE2_R), (BOSS4, HOLE4_R)):
    plate = plate.cut(cyl(xy, hr, -1, TOP + 2))
    plate = plate.cut(cyl(xy, UNDER_CB_R, -1, UNDER_CB_D + 1))
plate = plate.cut(cyl(BOSS3, HOLE3_R, -1, TOP + 2))
plate = plate.cut(cone(BOSS3, HOLE3_R, CSK3_R + 0.5, TOP - (CSK3_R - HOLE3_R),
                       CSK3_R - HOLE3_R + 0.5))

# ---------------------------------------------------------------------------
# 45 deg chamfers on the tab ends
# ---------------------------------------------------------------------------
def end_cutter(p_a, p_b, run, height_from_top, z_top, span):
    """wedge that removes material above a 45 deg plane rising from the
    bottom end-line p_a-p_b inwards"""
    A = np.array(P(*p_a))
    B = np.array(P(*p_b))
    mid = (A + B) / 2
    along = (B - A) / np.linalg.norm(B - A)
    inward = np.array([-along[1], along[0]])
    # make inward point toward the plate (toward layout centre)
    to_c = -mid
    if np.dot(inward, to_c) < 0:
        inward = -inward
    h0 = z_top - height_from_top
    pl = cq.Plane(origin=(float(mid[0]), float(mid[1]), 0.0),
                  xDir=(float(inward[0]), float(inward[1]), 0.0),
                  normal=(float(along[0]), float(along[1]), 0.0))
    if pl.yDir.z < 0:
        pl = cq.Plane(origin=(float(mid[0]), float(mid[1]), 0.0),
                      xDir=(float(inward[0]), float(inward[1]), 0.0),
                      normal=(float(-along[0]), float(-along[1]), 0.0))
    w = (cq.Workplane(pl)
         .polyline([(-5.0, h0), (0.0, h0), (run, z_top), (run, z_top + 5.0),
                    (-5.0, z_top + 5.0)]).close()
         .extrude(span, both=True))
    return w


for pa, pb in TAB_ENDS:
    plate = plate.cut(end_cutter(pa, pb, TAB_CH_RUN, TAB_CH_H, T, 20.0 * S))

# ---------------------------------------------------------------------------
# Two grooves across the underside of the tail
# ---------------------------------------------------------------------------
A = np.array(P(*TAIL_END[0]))
B = np.array(P(*TAIL_END[1]))
mid = (A + B) / 2
along = (B - A) / np.linalg.norm(B - A)
inward = np.array([-along[1], along[0]])
if np.dot(inward, -mid) < 0:
    inward = -inward
ang = math.degrees(math.atan2(inward[1], inward[0]))
for k in range(2):
    d0 = GROOVE_END + k * (GROOVE_W + GROOVE_GAP)
    c = mid + inward * (d0 + GROOVE_W / 2)
    g = (cq.Workplane("XY", origin=(0, 0, -1.0))
         .center(float(c[0]), float(c[1]))
         .rect(GROOVE_W, 34.0 * S)
         .extrude(GROOVE_D + 1.0)
         .rotate((float(c[0]), float(c[1]), 0), (float(c[0]), float(c[1]), 1), ang))
    plate = plate.cut(g)

result = plate
